import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
W = 40.0          # across flats of the octagonal housing (X and Z)
CH = 7.6          # corner chamfer leg of the octagon (same leg used for all inner steps)
D = 12.3          # depth along Y (front face y=0, open back y=D)

# stepped opening at the back (+Y)
T1 = 1.62         # wall thickness at the lip (first step inset)
Y1 = 9.45         # level of first ledge
T2 = 3.35         # inset of second step
Y2 = 7.67         # level of second ledge (= top of contact cavity)
T3 = 4.65         # wall thickness of the contact cavity
FLOOR = 1.8       # floor (front wall) thickness

# contacts
PIN_D = 1.45
PIN_TOP = 7.6     # tip level of the long contacts
STUB_H = 0.3      # height of the flush (short) contacts above the floor

# polarising key in the (+X,-Z) corner: a round bar cantilevered from the chamfer wall
KEY_ROD = 1.6     # bar diameter
KEY_BORE = 1.1    # bore of the bar (open towards the centre)
KEY_SLIT = 0.8    # width of the slit along the bar
KEY_Y = 7.0       # bar axis level
KEY_END = (0.8, -2.63)   # inner end of the key (XZ)
KEY_ANG = -39.0          # direction from the inner end towards the corner wall (deg)
KEY_L = 14.6      # bar length (runs a little into the chamfer wall)
KEY_OPEN = 13.9   # length of the bore / slit (up to the wall face)

# spring wires
WIRE_D = 0.7
WIRE_Y = 6.6

VIEW = {"azimuth": 45, "elevation": 26}


def octagon(w, c):
    h = w / 2.0
    return [
        (-h + c, -h), (h - c, -h), (h, -h + c), (h, h - c),
        (h - c, h), (-h + c, h), (-h, h - c), (-h, -h + c),
    ]


def oct_prism(inset, y0, y1):
    """Octagonal prism inset from the outside by `inset`, same chamfer leg, from y0 to y1."""
    w = W - 2 * inset
    wp = cq.Workplane("XZ", origin=(0, y0, 0)).polyline(octagon(w, CH)).close()
    return wp.extrude(-(y1 - y0))


def pin(x, z, y0, y1, d=PIN_D):
    return (cq.Workplane("XZ", origin=(0, y0, 0)).center(x, z)
            .circle(d / 2.0).extrude(-(y1 - y0)))


# ---------------- housing with stepped opening ----------------
body = oct_prism(0, 0, D)
body = body.cut(oct_prism(T1, Y1, D + 1))
body = body.cut(oct_prism(T2, Y2, D + 1))
body = body.cut(oct_prism(T3, FLOOR, D + 1))

# ---------------- contacts ----------------
long_pins = [(0.0, 13.8), (0.0, -13.8), (0.0, 6.15), (0.0, -6.15),
             (13.5, 0.0), (-13.5, 0.0), (5.95, 0.0), (-5.95, 0.0)]
for sx in (1, -1):
    for sz in (1, -1):
        for (px, pz) in [(7.0, 11.45), (4.58, 10.8), (11.3, 7.05), (10.6, 4.63)]:
            long_pins.append((sx * px, sz * pz))

short_pins = []
for sx in (1, -1):
    for sz in (1, -1):
        for (px, pz) in [(3.08, 3.05), (13.57, 4.21), (4.7, 13.85)]:
            short_pins.append((sx * px, sz * pz))

for (px, pz) in long_pins:
    body = body.union(pin(px, pz, FLOOR - 0.2, PIN_TOP))
for (px, pz) in short_pins:
    body = body.union(pin(px, pz, FLOOR - 0.2, FLOOR + STUB_H))

# ---------------- polarising key ----------------
ka = math.radians(KEY_ANG)
kdir = cq.Vector(math.cos(ka), 0, math.sin(ka))
kstart = cq.Vector(KEY_END[0], KEY_Y, KEY_END[1])
rod = cq.Solid.makeCylinder(KEY_ROD / 2.0, KEY_L, kstart, kdir)
bore = cq.Solid.makeCylinder(KEY_BORE / 2.0, KEY_OPEN, kstart - kdir * 0.01, kdir)
# longitudinal slit on the open (+Y) side of the bar, like a slotted spring pin
smid = kstart + kdir * (KEY_OPEN / 2.0)
slit = (cq.Workplane("XZ", origin=(0, KEY_Y, 0))
        .center(smid.x, smid.z)
        .rect(KEY_OPEN, KEY_SLIT)
        .extrude(-KEY_ROD)
        .rotate((smid.x, 0, smid.z), (smid.x, 1, smid.z), -KEY_ANG))
body = (body.union(cq.Workplane().add(rod))
        .cut(cq.Workplane().add(bore))
        .cut(slit))


# ---------------- spring wires ----------------
def wire(points, d=WIRE_D, y=WIRE_Y):
    """Round wire of diameter d swept along a polyline lying in the plane Y=y."""
    pts = [cq.Vector(x, y, z) for (x, z) in points]
    path = cq.Workplane("XY").polyline([(p.x, p.y, p.z) for p in pts])
    d0 = (pts[1] - pts[0]).normalized()
    plane = cq.Plane(origin=pts[0], xDir=d0.cross(cq.Vector(0, 1, 0)), normal=d0)
    return cq.Workplane(plane).circle(d / 2.0).sweep(path, transition="round")


w1 = wire([(11.7, 11.5), (12.35, 10.55), (11.21, 9.74), (0.58, 9.33)])
w2 = wire([(-11.2, -1.9), (-9.09, -5.22), (-9.09, -10.36), (-10.6, -12.55)])
body = body.union(w1).union(w2)

result = body
